import cadquery as cq

# ---- driving dimensions (mm) ----
base_d = 200.0        # bottom flange (base plate) diameter
base_t = 12.0         # bottom flange thickness
body_od = 131.3       # tube outer diameter
body_id = 116.0       # tube bore diameter
height = 242.3        # overall height
top_d = 158.0         # top flange diameter
top_t = 7.3           # top flange thickness
hole_r = 72.5         # bolt circle radius of top-flange pin holes
hole_d = 6.5          # pin hole diameter
hole_depth = 5.0      # blind pin hole depth
n_holes = 4
hole_start = 0.0      # angle of the first pin hole (deg, from +X)
seam_angle = 45.0     # where the cylindrical face seams end up (cosmetic)

# bottom flange (closed base plate)
base = cq.Workplane("XY").circle(base_d / 2).extrude(base_t)

# tube body
body = (cq.Workplane("XY").workplane(offset=base_t)
        .circle(body_od / 2).extrude(height - base_t - top_t))

# top flange
top = (cq.Workplane("XY").workplane(offset=height - top_t)
       .circle(top_d / 2).extrude(top_t))

part = base.union(body).union(top)

# bore, closed at the base plate
bore = (cq.Workplane("XY").workplane(offset=base_t)
        .circle(body_id / 2).extrude(height))
part = part.cut(bore)

# blind pin holes in the top flange face, 4x at 90 deg spacing
holes = (cq.Workplane("XY").workplane(offset=height - hole_depth)
         .polarArray(hole_r, hole_start - seam_angle, 360, n_holes)
         .circle(hole_d / 2).extrude(hole_depth + 1))
part = part.cut(holes)

# turn the axisymmetric body so the circle seams sit at seam_angle;
# the pin holes end up at hole_start + k*90 deg
result = part.rotate((0, 0, 0), (0, 0, 1), seam_angle)
